import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
DISC_R = 30.0          # hub disc radius
DISC_T = 8.5           # hub disc thickness (along Y)
ARM_D = 16.5           # arm depth along Y (front flush with disc front)
R_OUT = 58.6           # arm tips lie on this radius (arc end faces)
ARM_W = 8.0            # arm shaft width
FLARE_W = 20.0         # width of the flared arm end (45 deg flare)
TAPER_R0 = 24.4        # radius where the back rib taper meets the disc back face
ARM_EDGE_R = 2.0       # fillet on the arm's long edges
ARM_NECK_R = 2.0       # fillet at the flare / shaft junction
ROOT_R = 1.5           # fillet where the arms meet the disc rim

CENTER_HOLE_D = 12.0   # central through hole
BOLT_D = 6.4           # bolt through holes
CSK_D = 11.0           # countersink diameter on the front face
CSK_ANGLE = 90.0       # countersink included angle
BOLT_R_A = 19.5        # bolt radius on the 135/315 deg diagonal
BOLT_R_B = 16.5        # bolt radius on the 45/225 deg diagonal

Y_FRONT = -ARM_D / 2.0           # front (-Y) face of disc and arms
Y_DISC_BACK = Y_FRONT + DISC_T   # back face of disc
Y_ARM_BACK = Y_FRONT + ARM_D     # back face of arms


class _FnSel(cq.Selector):
    """Small helper selector driven by a predicate."""

    def __init__(self, fn):
        self.fn = fn

    def filter(self, objs):
        return [o for o in objs if self.fn(o)]


def _pts(e, n=5):
    return [e.positionAt(i / (n - 1)) for i in range(n)]


def _is_y_parallel(e):
    d = e.endPoint() - e.startPoint()
    return d.Length > 1e-6 and abs(d.y) / d.Length > 0.99


# ---------------- hub disc ----------------
disc = (
    cq.Workplane("XZ", origin=(0, Y_DISC_BACK, 0))
    .circle(DISC_R)
    .extrude(DISC_T)
)

# ---------------- one arm (pointing +Z) ----------------
a = ARM_W / 2.0
b = FLARE_W / 2.0
r_c = math.sqrt(R_OUT ** 2 - b ** 2)   # flare corner position
r_f0 = r_c - (b - a)                   # 45 deg flare starts here
ARM_Z0 = 20.0                          # arm solid starts inside the disc

arm = (
    cq.Workplane("XZ", origin=(0, Y_ARM_BACK, 0))
    .moveTo(-a, ARM_Z0)
    .lineTo(a, ARM_Z0)
    .lineTo(a, r_f0)
    .lineTo(b, r_c)
    .threePointArc((0, R_OUT), (-b, r_c))
    .lineTo(-a, r_f0)
    .close()
    .extrude(ARM_D)
)

# concave flare / shaft junction edges (parallel to Y)
arm = arm.edges("|Y").edges(
    cq.selectors.BoxSelector((-a - 0.1, -50, r_f0 - 0.1), (a + 0.1, 50, r_f0 + 0.1))
).fillet(ARM_NECK_R)

# back rib: 45 deg taper down onto the disc back face
rise = ARM_D - DISC_T
cutter = (
    cq.Workplane("YZ", origin=(-b - 2, 0, 0))
    .polyline([
        (Y_DISC_BACK, -5.0),
        (Y_DISC_BACK, TAPER_R0),
        (Y_ARM_BACK + 1.0, TAPER_R0 + rise + 1.0),
        (Y_ARM_BACK + 1.0, -5.0),
    ])
    .close()
    .extrude(FLARE_W + 4)
)
arm = arm.cut(cutter)

# root fillet filler: 2D fillet between the arm side (x = a) and the disc rim
f_cx = a + ROOT_R
f_cz = math.sqrt((DISC_R + ROOT_R) ** 2 - f_cx ** 2)
f_s = DISC_R / (DISC_R + ROOT_R)
f_xc, f_zc = f_cx * f_s, f_cz * f_s                  # tangent point on the rim
f_a0 = math.pi                                       # tangent point on arm side
f_a1 = math.atan2(f_zc - f_cz, f_xc - f_cx) + 2 * math.pi
f_am = 0.5 * (f_a0 + f_a1)
f_mx, f_mz = f_cx + ROOT_R * math.cos(f_am), f_cz + ROOT_R * math.sin(f_am)
f_zlo = f_zc - 3.0


def _root_filler(sign):
    return (
        cq.Workplane("XZ", origin=(0, Y_DISC_BACK, 0))
        .moveTo(sign * (a - 0.5), f_zlo)
        .lineTo(sign * (a - 0.5), f_cz)
        .lineTo(sign * a, f_cz)
        .threePointArc((sign * f_mx, f_mz), (sign * f_xc, f_zc))
        .lineTo(sign * f_xc, f_zlo)
        .close()
        .extrude(DISC_T)
    )


arm = arm.union(_root_filler(1)).union(_root_filler(-1)).clean()


# rounded long edges on the front and back faces of the arm
def _front_back_edge(e):
    if _is_y_parallel(e):
        return False
    if e.geomType() == "CIRCLE" and abs(e.radius() - R_OUT) < 0.01:
        return False                      # arc end faces keep sharp edges
    pts = _pts(e)
    rs = [math.hypot(p.x, p.z) for p in pts]
    if all(abs(p.y - Y_FRONT) < 1e-3 for p in pts) and min(rs) > DISC_R - 0.05:
        return True
    if all(abs(p.y - Y_ARM_BACK) < 1e-3 for p in pts):
        d = e.endPoint() - e.startPoint()
        if e.geomType() == "LINE" and abs(d.z) < 1e-6:
            return False                  # rib top edge stays sharp
        return True
    return False


arm = arm.edges(_FnSel(_front_back_edge)).fillet(ARM_EDGE_R)

# ---------------- combine hub + 4 arms ----------------
body = disc
for ang in (0, 90, 180, 270):
    body = body.union(arm.rotate((0, 0, 0), (0, 1, 0), ang))
body = body.clean()


# round the edges of the 45 deg rib taper
def _taper_edge(e):
    if e.geomType() != "LINE":
        return False
    d = e.endPoint() - e.startPoint()
    if d.Length < 1e-6:
        return False
    if abs(abs(d.y) - d.Length / math.sqrt(2)) < 0.05 * d.Length:
        return True                       # taper side edges
    pts = _pts(e, 3)
    if all(abs(p.y - Y_ARM_BACK) < 1e-3 for p in pts):
        rs = [math.hypot(p.x, p.z) for p in pts]
        if min(rs) < TAPER_R0 + rise + 0.5:
            return True                   # taper top edge
    return False


body = body.edges(_FnSel(_taper_edge)).fillet(ARM_EDGE_R)

# ---------------- holes ----------------
pts = []
for r, ang in ((BOLT_R_A, 135), (BOLT_R_A, 315), (BOLT_R_B, 45), (BOLT_R_B, 225)):
    pts.append((r * math.cos(math.radians(ang)), r * math.sin(math.radians(ang))))

center_cut = (
    cq.Workplane("XZ", origin=(0, Y_ARM_BACK + 1, 0))
    .circle(CENTER_HOLE_D / 2)
    .extrude(ARM_D + 2)
)
bolt_cut = (
    cq.Workplane("XZ", origin=(0, Y_ARM_BACK + 1, 0))
    .pushPoints(pts)
    .circle(BOLT_D / 2)
    .extrude(ARM_D + 2)
)
# 90 deg countersinks on the front face
csk_extra = 0.5
csk_r1 = CSK_D / 2 + csk_extra * math.tan(math.radians(CSK_ANGLE / 2))
csk_h = csk_r1 / math.tan(math.radians(CSK_ANGLE / 2))
csk_cut = None
for (px, pz) in pts:
    cone = cq.Solid.makeCone(
        csk_r1, 0.0, csk_h,
        cq.Vector(px, Y_FRONT - csk_extra, pz), cq.Vector(0, 1, 0),
    )
    csk_cut = cone if csk_cut is None else csk_cut.fuse(cone)

result = body.cut(center_cut).cut(bolt_cut).cut(cq.Workplane("XY").add(csk_cut))

VIEW = {"azimuth": 45, "elevation": 26}
